import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BASE_W = 36.6      # X
BASE_D = 41.8      # Y
BASE_H = 40.15     # Z

CAP_W = 31.45      # cap size in X (flush with -X side of base)
CAP_D = 31.45      # cap size in Y (centred in Y)
CAP_H = 17.5       # cap height above base top
CAP_R_VERT = 3.5   # vertical edge rounding of cap
CAP_R_TOP = 3.2    # top edge rounding of cap

# power symbol (raised)
SYM_H = 1.75           # emboss height
RING_RO = 11.05       # ring outer radius
RING_RI = 8.1          # ring inner radius
GAP_HALF = 41.0        # half angle of C gap (deg, around +Y)
STICK_W = 3.0          # stick width
STICK_Y0 = -1.64       # stick lower end (relative to cap centre)
STICK_Y1 = 11.75       # stick upper end

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- base block ----------------
base = cq.Workplane("XY").box(BASE_W, BASE_D, BASE_H, centered=(True, True, False))

# ---------------- cap ----------------
cap_cx = -BASE_W / 2 + CAP_W / 2
cap_cy = 0.0
cap = (
    cq.Workplane("XY")
    .workplane(offset=BASE_H)
    .center(cap_cx, cap_cy)
    .rect(CAP_W, CAP_D)
    .extrude(CAP_H)
    .edges("|Z").fillet(CAP_R_VERT)
    .faces(">Z").edges().fillet(CAP_R_TOP)
)

body = base.union(cap)

# ---------------- power symbol ----------------
top_z = BASE_H + CAP_H
rc = 0.5 * (RING_RO + RING_RI)
hw = 0.5 * (RING_RO - RING_RI)
t1 = math.radians(90 + GAP_HALF)        # start of C (left end)
t2 = math.radians(90 - GAP_HALF + 360)  # end of C (right end)


def pol(r, t):
    return (cap_cx + r * math.cos(t), cap_cy + r * math.sin(t))


e2 = pol(rc, t2)
e1 = pol(rc, t1)
cap2_mid = (e2[0] - hw * math.sin(t2), e2[1] + hw * math.cos(t2))
cap1_mid = (e1[0] + hw * math.sin(t1), e1[1] - hw * math.cos(t1))

ring = (
    cq.Workplane("XY")
    .workplane(offset=top_z)
    .moveTo(*pol(RING_RO, t1))
    .threePointArc(pol(RING_RO, math.radians(270)), pol(RING_RO, t2))
    .threePointArc(cap2_mid, pol(RING_RI, t2))
    .threePointArc(pol(RING_RI, math.radians(270)), pol(RING_RI, t1))
    .threePointArc(cap1_mid, pol(RING_RO, t1))
    .close()
    .extrude(SYM_H)
)

stick_len = STICK_Y1 - STICK_Y0
stick = (
    cq.Workplane("XY")
    .workplane(offset=top_z)
    .center(cap_cx, cap_cy + 0.5 * (STICK_Y0 + STICK_Y1))
    .slot2D(stick_len, STICK_W, angle=90)
    .extrude(SYM_H)
)

result = body.union(ring).union(stick)
